import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
MODULE = 2.0          # gear module
N_TEETH = 32          # number of teeth
PRESSURE_ANGLE = 20.0 # degrees
ADDENDUM = 1.0 * MODULE
DEDENDUM = 1.25 * MODULE

GEAR_THICK = 8.0      # overall face width (rim height)
WEB_THICK = 4.0       # thickness of recessed web
RIM_INNER_R = 27.0    # inner radius of the raised rim

COLLAR_D = 16.0       # short collar at the hub
COLLAR_TOP = 8.0      # z of collar top
COLLAR_FILLET = 1.25  # round on the collar top edge
SHAFT_D = 12.0        # hub / shaft diameter
SHAFT_TOP = 20.0      # z of shaft top
BORE_D = 4.0          # through bore

N_SLOTS = 6
SLOT_WIDTH = 8.0
SLOT_LENGTH = 16.0    # overall length (end to end)
SLOT_CENTER_R = 17.0  # radial position of slot centre
SLOT_START_ANGLE = 90.0

# ---------------- gear outline ----------------
r_pitch = MODULE * N_TEETH / 2.0
r_tip = r_pitch + ADDENDUM
r_root = r_pitch - DEDENDUM
alpha = math.radians(PRESSURE_ANGLE)
r_base = r_pitch * math.cos(alpha)


def inv(a):
    return math.tan(a) - a


half_tooth_pitch = math.pi / (2 * N_TEETH)  # half tooth thickness angle at pitch


def flank_angle(r):
    """polar half-angle of the tooth flank at radius r (tooth centred on 0)"""
    r = max(r, r_base)
    a_r = math.acos(r_base / r)
    return half_tooth_pitch + inv(alpha) - inv(a_r)


def polar(r, ang):
    return (r * math.cos(ang), r * math.sin(ang))


pitch_ang = 2 * math.pi / N_TEETH
N_FLANK = 5
r_start = max(r_base, r_root)
flank_r = [r_start + (r_tip - r_start) * (i / (N_FLANK - 1)) for i in range(N_FLANK)]

# outline: tip arc of each tooth, then one smooth curve through the
# involute flank, the rounded root and the next involute flank
wp = cq.Workplane("XY").moveTo(*polar(r_tip, -flank_angle(r_tip)))
for k in range(N_TEETH):
    c = k * pitch_ang
    cn = c + pitch_ang
    # tip land
    wp = wp.threePointArc(polar(r_tip, c), polar(r_tip, c + flank_angle(r_tip)))
    # tooth gap: left flank of tooth k down, root, right flank of tooth k+1 up
    pts = [polar(r, c + flank_angle(r)) for r in reversed(flank_r)][1:]
    pts.append(polar(r_root, c + 0.5 * pitch_ang))
    pts += [polar(r, cn - flank_angle(r)) for r in flank_r]
    wp = wp.spline(pts, includeCurrent=True)
wp = wp.close()
gear = wp.extrude(GEAR_THICK)

# ---------------- recess the web ----------------
recess = (
    cq.Workplane("XY")
    .workplane(offset=WEB_THICK)
    .circle(RIM_INNER_R)
    .extrude(GEAR_THICK)
)
gear = gear.cut(recess)

# ---------------- hub collar + shaft (revolved profile) ----------------
rc = COLLAR_D / 2
rs = SHAFT_D / 2
f = COLLAR_FILLET
hub_prof = (
    cq.Workplane("XZ")
    .moveTo(0, WEB_THICK - 0.5)
    .lineTo(rc, WEB_THICK - 0.5)
    .lineTo(rc, COLLAR_TOP - f)
    .threePointArc(
        (rc - f + f * math.cos(math.pi / 4), COLLAR_TOP - f + f * math.sin(math.pi / 4)),
        (rc - f, COLLAR_TOP),
    )
)
if rc - f > rs + 1e-6:
    hub_prof = hub_prof.lineTo(rs, COLLAR_TOP)
hub_prof = hub_prof.lineTo(rs, SHAFT_TOP).lineTo(0, SHAFT_TOP).close()
# revolve, then turn the seam to the back of the part
hub = hub_prof.revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 0, 1), 90)
gear = gear.union(hub)

# ---------------- lightening slots ----------------
slots = None
for i in range(N_SLOTS):
    ang = SLOT_START_ANGLE + i * 360.0 / N_SLOTS
    a = math.radians(ang)
    s = (
        cq.Workplane("XY")
        .workplane(offset=-1)
        .center(SLOT_CENTER_R * math.cos(a), SLOT_CENTER_R * math.sin(a))
        .slot2D(SLOT_LENGTH, SLOT_WIDTH, ang)
        .extrude(GEAR_THICK + 2)
    )
    slots = s if slots is None else slots.union(s)
gear = gear.cut(slots)

# ---------------- bore ----------------
bore = (
    cq.Workplane("XY")
    .workplane(offset=-1)
    .circle(BORE_D / 2)
    .extrude(SHAFT_TOP + 2)
)
gear = gear.cut(bore)

result = gear

VIEW = {"azimuth": 45, "elevation": 26}
